"""Offset duct / WC pan connector.

Vertical round socket on top (with a shallow recessed floor and a groove ring),
a neck that squeezes into a flat oval while swinging back (-Y), a tight 90 degree
elbow ending in a rounded boot, and a horizontal spigot outlet facing +Y with a
stepped collar and lip.  The neck and elbow are smooth lofts through a few
parametric oval sections; the boot end is a revolved half-ellipse (spheroid).
"""
import math
import cadquery as cq

V = cq.Vector

# ---------------- driving dimensions (mm) ----------------
D = 100.0                  # socket / body nominal diameter
R = D / 2.0
H_TOP = 219.3              # overall height (socket rim)
Z_GROOVE = 182.7           # groove ring on the socket = top of the shaped neck
GROOVE_W = 1.4
GROOVE_D = 0.7
SOCKET_WALL = 1.9          # rim wall thickness
SOCKET_DEPTH = 18.0        # depth of the socket recess
SOCKET_CHAMFER = 1.2       # chamfer round the socket floor

Z_OUT = 49.75              # outlet axis height
R_OB = 49.75               # radius of the round body at the outlet
Y_BODY_END = -19.3         # round body -> collar step
Y_LIP0 = -3.3              # collar -> lip step
Y_FACE = 0.0               # outlet face (in the socket axis plane)
R_COLLAR = 47.1
R_LIP = 43.5

# elbow: sections fanned about an axis parallel to X through (C_Y, C_Z)
R_THROAT = 2.0             # inner (throat) radius of the elbow
C_Y = -24.4
C_Z = Z_OUT + R_OB + R_THROAT

# boot end: half-ellipse revolved about the outlet axis (spheroid)
BOOT_YC = -44.25           # centre along Y
BOOT_ZC = 49.75            # centre height
BOOT_RY = 31.75            # reach along -Y
BOOT_R = 49.75             # radius about the outlet axis
BOOT_BLEND = 8.0            # fillet blending the boot into the elbow

# oval sections: four cubic Bezier quadrants.  k = handle factor of a quadrant
# (0.5523 = elliptic, larger = squarer, smaller = more pointed)
K_E = 0.5523
# neck (horizontal planes): z, half width X, front (+Y) extent, back (-Y) extent,
#                           y of the widest line, k front, k back
NECK = [
    (165.0, 49.4, 49.6, -50.3, 0.0, K_E, K_E),
    (148.0, 46.8, 46.9, -51.5, -14.475, 0.6129, 0.5912),
    (134.0, 46.1, 16.6, -53.6, -34.625, 0.5013, 0.5069),
    (120.0, 47.0, -18.0, -56.6, -34.775, 0.5523, 0.5823),
]
# elbow (planes through the bend axis, tilted theta below horizontal):
#   theta, outer reach from the bend axis, half width X, widest-line fraction,
#   k throat side, k outer side
ELBOW = [
    (0.0, 36.4, 48.1, 0.4, 0.5971, 0.5856),
    (30.0, 52.5, 48.0, 0.5, 0.4847, 0.4847),
    (55.0, 85.5, 46.0, 0.5, K_E, K_E),
]


def quadrant(p0, corner, p1, k):
    """cubic Bezier quarter from p0 to p1 bulging toward `corner`"""
    return cq.Edge.makeBezier([p0, p0 + (corner - p0) * k, p1 + (corner - p1) * k, p1])


def oval(c, ex, ey, a, bf, bb, kf=K_E, kb=K_E):
    """closed oval in the plane (ex, ey) about c: half width a along ex,
    reaching bf forward (+ey) and bb backward; C1 at the four axis points.
    Elliptic quadrants (k = K_E) are built as exact elliptical arcs."""
    n = ex.cross(ey)
    px, nx = c + ex * a, c - ex * a
    pf, pb = c + ey * bf, c - ey * bb

    def quarter(p0, corner, p1, k, b, ang):
        if abs(k - K_E) < 1e-9:
            return cq.Edge.makeEllipse(a, b, c, n, ex, ang, ang + 90)
        return quadrant(p0, corner, p1, k)

    return cq.Wire.assembleEdges([
        quarter(px, px + ey * bf, pf, kf, bf, 0),
        quarter(pf, nx + ey * bf, nx, kf, bf, 90),
        quarter(nx, nx - ey * bb, pb, kb, bb, 180),
        quarter(pb, px - ey * bb, px, kb, bb, 270),
    ])


def neck_section(z, a, y_front, y_back, y_wide, kf=K_E, kb=K_E):
    return oval(V(0, y_wide, z), V(1, 0, 0), V(0, 1, 0),
                a, y_front - y_wide, y_wide - y_back, kf, kb)


def elbow_section(theta, reach, a, frac, kf=K_E, kb=K_E):
    t = math.radians(theta)
    d = V(0, -math.cos(t), -math.sin(t))          # away from the bend axis
    s_wide = R_THROAT + frac * (reach - R_THROAT)
    c = V(0, C_Y, C_Z) + d * s_wide
    return oval(c, V(1, 0, 0), -d, a, s_wide - R_THROAT, reach - s_wide, kf, kb)


# ---------------- neck + elbow lofts ----------------
elbow_wires = [elbow_section(*s) for s in ELBOW] + \
    [elbow_section(90.0, C_Z - (Z_OUT - R_OB), R_OB, 0.5)]     # round outlet end
neck_wires = [neck_section(Z_GROOVE, R, R, -R, 0.0)] + \
    [neck_section(*s) for s in NECK] + [elbow_wires[0]]

# the neck is lofted in two runs (split at the third section) so the steep
# squeeze of the front wall does not make the upper part ripple
N_SPLIT = 2
neck = (cq.Workplane("XY").add(cq.Solid.makeLoft(neck_wires[:N_SPLIT + 1]))
        .union(cq.Workplane("XY").add(cq.Solid.makeLoft(neck_wires[N_SPLIT:]))))
elbow = cq.Workplane("XY").add(cq.Solid.makeLoft(elbow_wires))

# ---------------- rounded boot end ----------------
# a sphere stretched into a spheroid (radius BOOT_R about the outlet axis,
# reaching BOOT_RY along -Y)
boot = cq.Workplane("XY").add(
    cq.Solid.makeSphere(1.0, angleDegrees1=-90, angleDegrees2=90).transformGeometry(
        cq.Matrix([[BOOT_R, 0, 0, 0], [0, BOOT_RY, 0, BOOT_YC], [0, 0, BOOT_R, BOOT_ZC]])))

# ---------------- socket ----------------
socket = (cq.Workplane("XY").workplane(offset=Z_GROOVE)
          .circle(R).extrude(H_TOP - Z_GROOVE))


# ---------------- outlet: short round body, collar, lip ----------------
def y_cylinder(radius, y0, y1):
    return (cq.Workplane("XZ", origin=(0, y0, Z_OUT))
            .circle(radius).extrude(-(y1 - y0)))


outlet = (y_cylinder(R_OB, C_Y, Y_BODY_END)
          .union(y_cylinder(R_COLLAR, Y_BODY_END, Y_LIP0))
          .union(y_cylinder(R_LIP, Y_LIP0, Y_FACE)))

part = socket.union(neck).union(elbow).union(boot).union(outlet)


def on_boot(p, tol=1e-3):
    return abs((p.x / BOOT_R) ** 2 + ((p.y - BOOT_YC) / BOOT_RY) ** 2
               + ((p.z - BOOT_ZC) / BOOT_R) ** 2 - 1.0) < tol


# blend the boot into the elbow: fillet the boot face's boundary
boot_faces = [f for f in part.faces().vals() if on_boot(f.positionAt(0.5, 0.5))]
blend_edges = [e for f in boot_faces for e in f.Edges()]
if blend_edges:
    try:
        part = cq.Workplane("XY").add(part.val().fillet(BOOT_BLEND, blend_edges))
    except Exception:
        pass

# ---------------- socket recess (chamfered floor) and groove ring ----------------
r_bore = R - SOCKET_WALL
recess = (cq.Workplane("XZ")
          .polyline([(0, H_TOP + 1), (r_bore, H_TOP + 1),
                     (r_bore, H_TOP - SOCKET_DEPTH + SOCKET_CHAMFER),
                     (r_bore - SOCKET_CHAMFER, H_TOP - SOCKET_DEPTH),
                     (0, H_TOP - SOCKET_DEPTH)])
          .close()
          .revolve(360, (0, 0, 0), (0, 1, 0)))
part = part.cut(recess)

groove = (cq.Workplane("XY").workplane(offset=Z_GROOVE - GROOVE_W / 2)
          .circle(R + 1).circle(R - GROOVE_D).extrude(GROOVE_W))
part = part.cut(groove)

result = part
